import cadquery as cq
from cadquery import Vector as V
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakePipeShell
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRepPrimAPI import BRepPrimAPI_MakeCylinder, BRepPrimAPI_MakeCone, BRepPrimAPI_MakeSphere
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir, gp_Circ, gp_Elips

# =====================================================================
#  Exhaust / intake tube: long 3D-bent pipe with a flared bell inlet and
#  a cast manifold head (trunk, side branch with trumpet, ports, stubs)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
PIPE_R = 10.0            # main pipe outer radius
BELL_R = 16.5            # flared inlet bell radius
BELL_LEN = 12.0          # length of the bell flare
BELL_RIM = 2.0           # bell rim thickness
BELL_DISH = 5.0          # depth of the spherical dish in the bell face
BELL_DISH_R = 25.0       # radius of the dish sphere

SLEEVE_R = 11.0          # collar sleeve where the pipe enters the manifold
SLEEVE_LEN = 21.0

# trunk: elliptical section, tapering from the hub to the foot
TRUNK_A0, TRUNK_B0 = 15.0, 11.0   # semi-axes at the hub end
TRUNK_A1, TRUNK_B1 = 12.0, 7.5    # semi-axes at the foot end
TRUNK_MAJOR = (0.66, 0.66, 0.37)  # direction of the wide axis

TRUMPET_NECK_R = 9.0     # trumpet neck radius
TRUMPET_MOUTH_R = 15.0   # trumpet mouth radius


# main pipe centreline (x, y, z), from the flared inlet to the manifold collar
PIPE_PTS = [
    (50, -574, -74),
    (42.8, -565.6, -78.6),
    (30, -540, -82),
    (16, -495, -84),
    (14, -460, -75),
    (25, -410, -58),
    (50, -350, -26),
    (85, -285, 20),
    (108, -230, 62),
    (118, -170, 100),
    (120, -100, 118),
    (118, -40, 122),
    (110, 25, 121),
    (93, 90, 114),
    (72, 160, 106),
    (50, 230, 96),
    (20, 305, 82),
    (-16, 389, 65),
]

# manifold trunk centreline (starts inside the collar sleeve)
TRUNK_PTS = [
    (-26, 404, 62),
    (-36, 420, 52),
    (-47, 444, 32),
    (-56, 483, 8),
    (-67, 521, -18),
    (-78, 550, -46),
    (-88, 564, -66),
]
HUB_C, HUB_R = (-38, 415, 48), 14.0

# side branch: loft from an ellipse inside the hub to one at the outer end
BR_IN_C, BR_IN_RY, BR_IN_RZ = (-42, 410, 37), 16.0, 16.5
BR_OUT_C, BR_OUT_RY, BR_OUT_RZ = (-96, 403, 31), 16.0, 17.0

BR_KNUCKLE_C, BR_KNUCKLE_R = (-102, 399, 26), 15.0   # bulky casting node joining the lobes

# trumpet (front-left lobe): neck centre -> mouth centre
TRUMPET_NECK, TRUMPET_MOUTH = (-98, 378, 18), (-122, 359, 14)
# rear stub (back-left lobe)
REAR_STUB_A, REAR_STUB_B, REAR_STUB_R = (-92, 414, 14), (-123, 422, 4), 10.0
# cylinder-head port on the front face (bored), and the round flange below it
UP_PORT_A, UP_PORT_B, UP_PORT_R, UP_PORT_BORE = (-86, 398, 31), (-88, 356, 38), 12.5, 8.5
FLANGE_C, FLANGE_N, FLANGE_R, FLANGE_T = (-85.5, 383.5, 18.5), (0.58, -0.58, -0.57), 20.0, 5.0

# trunk stubs, foot, spike and outlet
STUB1_A, STUB1_B, STUB1_R = (-66, 536, -40), (-114, 535, -40), 13.0
STUB2_A, STUB2_B, STUB2_R = (-92, 568, -82), (-114, 570, -88), 8.0
DUCT_A, DUCT_B = (-92, 566, -68), (-73, 585, -106)   # flared duct to the outlet
DUCT_R0, DUCT_R1 = 11.5, 15.0
SPIKE_BASE, SPIKE_TIP, SPIKE_R = (-82, 578, -98), (-88.5, 575, -127), 7.0

# seams of revolved faces are placed on the side facing away from the default camera
HIDDEN = V(-0.636, 0.636, -0.438)


def vec(p):
    return V(*p) if not isinstance(p, V) else p


def ax2(p, d, xdir=HIDDEN):
    p, d, xd = vec(p), vec(d).normalized(), vec(xdir)
    xd = xd - d * xd.dot(d)
    if xd.Length < 1e-6:
        xd = V(0, 0, 1) - d * d.z
        if xd.Length < 1e-6:
            xd = V(1, 0, 0) - d * d.x
    xd = xd.normalized()
    return gp_Ax2(gp_Pnt(p.x, p.y, p.z), gp_Dir(d.x, d.y, d.z), gp_Dir(xd.x, xd.y, xd.z))


def spline(pts):
    return cq.Edge.makeSpline([vec(p) for p in pts])


def section(p, t, a, b, xdir):
    """Closed circle (a == b) or ellipse in the plane normal to t, wide axis along xdir."""
    ax = ax2(p, t, xdir)
    if abs(a - b) < 1e-9:
        e = BRepBuilderAPI_MakeEdge(gp_Circ(ax, a)).Edge()
    else:
        e = BRepBuilderAPI_MakeEdge(gp_Elips(ax, a, b)).Edge()
    return cq.Wire.assembleEdges([cq.Edge(e)])


def sweep(path, r0, r1=None, xdir=HIDDEN):
    """Tube swept along a smooth 3D spline (discrete trihedron: no twist).
    r0 / r1 are radii or (a, b) ellipse semi-axes at the start / end of the path."""
    r0 = r0 if isinstance(r0, tuple) else (r0, r0)
    builder = BRepOffsetAPI_MakePipeShell(cq.Wire.assembleEdges([path]).wrapped)
    builder.SetDiscreteMode()
    builder.Add(section(path.startPoint(), path.tangentAt(0), r0[0], r0[1], xdir).wrapped, False, False)
    if r1 is not None:
        r1 = r1 if isinstance(r1, tuple) else (r1, r1)
        builder.Add(section(path.endPoint(), path.tangentAt(1), r1[0], r1[1], xdir).wrapped, False, False)
    builder.Build()
    builder.MakeSolid()
    return cq.Shape.cast(builder.Shape())


def cyl(p, d, r, h):
    return cq.Shape.cast(BRepPrimAPI_MakeCylinder(ax2(p, d), r, h).Shape())


def cone(p, d, r1, r2, h):
    return cq.Shape.cast(BRepPrimAPI_MakeCone(ax2(p, d), r1, r2, h).Shape())


def rod(a, b, r):
    a, b = vec(a), vec(b)
    return cyl(a, b - a, r, (b - a).Length)


def sphere(p, r, axis=(0, 0, 1), xdir=HIDDEN):
    return cq.Shape.cast(BRepPrimAPI_MakeSphere(ax2(p, axis, xdir), r).Shape())

# ---------------- main pipe with flared bell inlet ----------------
pipe_path = spline(PIPE_PTS)
body = sweep(pipe_path, PIPE_R, xdir=(0, 0, -1))

p0 = pipe_path.startPoint()
t0 = pipe_path.tangentAt(0)          # points into the pipe
bell_face = p0 - t0 * BELL_LEN       # centre of the bell's open face
bell = cone(p0 + t0 * 1.0, -t0, PIPE_R, BELL_R, BELL_LEN + 1.0)
rim = cyl(bell_face, t0, BELL_R + 0.8, BELL_RIM)
side = t0.cross(V(0, 0, 1)).normalized()
dish = sphere(bell_face - t0 * (BELL_DISH_R - BELL_DISH), BELL_DISH_R, side, -t0)
body = body.fuse(bell).fuse(rim).cut(dish)

# ---------------- manifold collar sleeve ----------------
p1 = pipe_path.endPoint()
t1 = pipe_path.tangentAt(1)
sleeve = cyl(p1 - t1 * 1.0, t1, SLEEVE_R, SLEEVE_LEN)
body = body.fuse(sleeve)

# ---------------- manifold trunk (tapered elliptical sweep) ----------------
trunk = sweep(spline(TRUNK_PTS), (TRUNK_A0, TRUNK_B0), (TRUNK_A1, TRUNK_B1), xdir=TRUNK_MAJOR)
body = body.fuse(trunk).fuse(sphere(HUB_C, HUB_R))

# ---------------- side branch body (lofted between two ellipses) ----------------
br_in = cq.Wire.makeEllipse(BR_IN_RY, BR_IN_RZ, vec(BR_IN_C), V(-1, 0, 0), V(0, 1, 0))
br_out = cq.Wire.makeEllipse(BR_OUT_RY, BR_OUT_RZ, vec(BR_OUT_C), V(-1, 0, 0), V(0, 1, 0))
body = body.fuse(cq.Solid.makeLoft([br_in, br_out]))
body = body.fuse(sphere(BR_KNUCKLE_C, BR_KNUCKLE_R))

# trumpet with a dished mouth
tn, tm = vec(TRUMPET_NECK), vec(TRUMPET_MOUTH)
td = (tm - tn).normalized()
tl = (tm - tn).Length
trumpet = cone(tn - td * 6.0, td, TRUMPET_NECK_R, TRUMPET_MOUTH_R, tl + 6.0)
tr_bore = cone(tm + td * 0.01, -td, TRUMPET_MOUTH_R - 1.5, TRUMPET_NECK_R - 3.0, 14.0)
body = body.fuse(trumpet).cut(tr_bore)

# rear stub
body = body.fuse(rod(REAR_STUB_A, REAR_STUB_B, REAR_STUB_R))

# bored port on the front face
pa, pb = vec(UP_PORT_A), vec(UP_PORT_B)
pd = (pb - pa).normalized()
body = body.fuse(rod(pa, pb, UP_PORT_R))
body = body.cut(cyl(pb - pd * 6.0, pd, UP_PORT_BORE, 7.0))

# round flange facing down / forward
fn = vec(FLANGE_N).normalized()
fc = vec(FLANGE_C)
body = body.fuse(cyl(fc - fn * 16.0, fn, FLANGE_R - 4.0, 12.0))
body = body.fuse(cyl(fc - fn * FLANGE_T, fn, FLANGE_R, FLANGE_T))

# ---------------- stubs, outlet duct and spike on the trunk ----------------
body = body.fuse(rod(STUB1_A, STUB1_B, STUB1_R))     # large side stub
body = body.fuse(sphere(DUCT_A, DUCT_R0))             # elbow into the duct
da, db = vec(DUCT_A), vec(DUCT_B)
dd = (db - da).normalized()
body = body.fuse(cone(da, dd, DUCT_R0, DUCT_R1, (db - da).Length))  # flared outlet duct
body = body.fuse(rod(STUB2_A, STUB2_B, STUB2_R))     # lower side stub
for (sa, sb_, sr) in ((STUB1_A, STUB1_B, STUB1_R), (STUB2_A, STUB2_B, STUB2_R)):
    s_a, s_b = vec(sa), vec(sb_)
    sd = (s_b - s_a).normalized()
    body = body.cut(cyl(s_b - sd * 8.0, sd, sr * 0.5, 9.0))   # bored stub ends
sb, st = vec(SPIKE_BASE), vec(SPIKE_TIP)
body = body.fuse(cone(sb, st - sb, SPIKE_R, 1.2, (st - sb).Length))  # spike
body = body.cut(cyl(db - dd * 8.0, dd, DUCT_R1 - 2.0, 10.0))          # open outlet bore

result = cq.Workplane("XY").add(body)
